import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 60.0            # overall width (X)
H = 16.5            # tall box height (Z)
BOX_WALL_Y = 58.5   # tall box +Y wall outer face
L = 118.5           # overall length (Y)

T_SIDE = 3.0        # tall box side wall thickness
T_FRONT = 2.7       # tall box front (-Y) wall thickness
T_BACK = 2.5        # tall box back (+Y) wall thickness
R_OUT = 4.7         # outer vertical corner radius (front of box)
R_IN = 2.5          # inner vertical corner radius of the tall box

EAR_A = 5.0         # ear gusset width at the back wall (X)
EAR_B = 4.0         # ear gusset length past the back wall (Y)

FZ0 = 4.45          # frame bottom
FZ1 = 11.35         # frame top
F_WALL = 2.2        # frame side wall thickness
F_END_WALL = 2.2    # frame far wall thickness
F_NEAR_IN = 61.0    # frame inner face on the box side
R_F_OUT = 5.0       # frame far outer corner radius
R_F_IN = 3.0        # frame inner corner radius

# tall box standoff tabs (hang from the walls)
TAB_TOP = 11.5
TAB_BOT = 6.0
TAB_A = dict(x=-16.0, y=15.0, r=3.3)   # on front wall, pointing +Y
TAB_B = dict(x=15.6, y=43.3, r=3.3)   # on +X wall, pointing -X
TAB_HOLE = 2.5      # threaded hole, modelled plain

# slot through the back wall
SLOT_LEN = 30.6
SLOT_H = 2.8
SLOT_Z = 8.1
SLOT_X = 0.0

# frame corner bosses
BOSS_X = 19.9
BOSS_W = 4.6
BOSS_LEN = 6.1      # from the wall inner face
BOSS_ROOT = 1.4     # how far the boss runs into the wall
BOSS_TOP = 8.0
BOSS_BOT = 3.0
BOSS_R = 1.0
BOSS_CH_V = 1.4     # bottom chamfer on the free end: vertical leg
BOSS_CH_H = 0.8     # bottom chamfer on the free end: horizontal leg
BOSS_HOLE = 2.0
BOSS_HOLE_OFF = 3.3

# rebates in the frame walls near the corners
REB_DEPTH = 1.0
REB_Z = BOSS_TOP + 1.0   # rebate floor
REB_SLOPE = 1.3          # sloped run from the boss top up to the rebate floor
REB_X_END = 16.6    # |X| where the rebate along the Y walls ends
REB_Y_LEN = 8.3     # rebate length along the X walls (from the Y wall)

# V notch in the +X frame wall
NOTCH_Y = 105.3
NOTCH_TOP_W = 9.0
NOTCH_BOT_W = 6.0
NOTCH_D = 2.0

hw = W / 2.0

# ---------------- tall box ----------------
box = (
    cq.Workplane("XY")
    .center(0, BOX_WALL_Y / 2.0)
    .rect(W, BOX_WALL_Y)
    .extrude(H)
    .edges("|Z and <Y")
    .fillet(R_OUT)
)
inner = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .center(0, (T_FRONT + BOX_WALL_Y - T_BACK) / 2.0)
    .rect(W - 2 * T_SIDE, BOX_WALL_Y - T_BACK - T_FRONT)
    .extrude(H + 2)
    .edges("|Z")
    .fillet(R_IN)
)
box = box.cut(inner)

# ear gussets: side walls continue past the back wall with a concave sweep
for sx in (-1, 1):
    x0 = sx * hw
    xa = sx * (hw - EAR_A)
    blk = (
        cq.Workplane("XY")
        .center((x0 + xa) / 2.0, BOX_WALL_Y + EAR_B / 2.0 - 0.25)
        .rect(EAR_A, EAR_B + 0.5)
        .extrude(H)
    )
    ell = (
        cq.Workplane("XY")
        .workplane(offset=-1)
        .center(xa, BOX_WALL_Y + EAR_B)
        .ellipse(EAR_A, EAR_B)
        .extrude(H + 2)
    )
    box = box.union(blk.cut(ell))

# ---------------- thin frame ----------------
f_len = L - BOX_WALL_Y
frame = (
    cq.Workplane("XY")
    .workplane(offset=FZ0)
    .center(0, BOX_WALL_Y + f_len / 2.0)
    .rect(W, f_len)
    .extrude(FZ1 - FZ0)
    .edges("|Z and >Y")
    .fillet(R_F_OUT)
)
f_far_in = L - F_END_WALL
f_in_len = f_far_in - F_NEAR_IN
frame_in = (
    cq.Workplane("XY")
    .workplane(offset=FZ0 - 1)
    .center(0, F_NEAR_IN + f_in_len / 2.0)
    .rect(W - 2 * F_WALL, f_in_len)
    .extrude(FZ1 - FZ0 + 2)
    .edges("|Z")
    .fillet(R_F_IN)
)
frame = frame.cut(frame_in)

body = box.union(frame)

# ---------------- hanging standoff tabs in the tall box ----------------
def tab_y(x, y, r, y_wall):
    """tab attached to a wall at y_wall, rounded end centred on (x, y)"""
    length = y - y_wall
    t = (
        cq.Workplane("XY")
        .workplane(offset=TAB_BOT)
        .center(x, y_wall + length / 2.0)
        .rect(2 * r, length)
        .extrude(TAB_TOP - TAB_BOT)
    )
    c = (
        cq.Workplane("XY")
        .workplane(offset=TAB_BOT)
        .center(x, y)
        .circle(r)
        .extrude(TAB_TOP - TAB_BOT)
    )
    return t.union(c)


def tab_x(x, y, r, x_wall):
    length = x_wall - x
    t = (
        cq.Workplane("XY")
        .workplane(offset=TAB_BOT)
        .center(x + length / 2.0, y)
        .rect(length, 2 * r)
        .extrude(TAB_TOP - TAB_BOT)
    )
    c = (
        cq.Workplane("XY")
        .workplane(offset=TAB_BOT)
        .center(x, y)
        .circle(r)
        .extrude(TAB_TOP - TAB_BOT)
    )
    return t.union(c)


ta = tab_y(TAB_A["x"], TAB_A["y"], TAB_A["r"], T_FRONT - 0.5)
tb = tab_x(TAB_B["x"], TAB_B["y"], TAB_B["r"], hw - T_SIDE + 0.5)
body = body.union(ta).union(tb)
for (hx, hy) in [(TAB_A["x"], TAB_A["y"]), (TAB_B["x"], TAB_B["y"])]:
    body = body.cut(
        cq.Workplane("XY").workplane(offset=TAB_BOT - 1).center(hx, hy)
        .circle(TAB_HOLE / 2).extrude(TAB_TOP - TAB_BOT + 2)
    )

# ---------------- slot through the back wall ----------------
slot = (
    cq.Workplane("XY")
    .workplane(offset=SLOT_Z - SLOT_H / 2.0)
    .center(SLOT_X, (BOX_WALL_Y - T_BACK + F_NEAR_IN) / 2.0)
    .rect(SLOT_LEN, F_NEAR_IN - BOX_WALL_Y + T_BACK + 2)
    .extrude(SLOT_H)
)
body = body.cut(slot)

# ---------------- frame wall rebates near the corners ----------------
# the inner contour of the frame, grown by REB_DEPTH, is cut down to the
# rebate floor inside a box around each corner
reb_outline = (
    cq.Workplane("XY")
    .workplane(offset=REB_Z)
    .center(0, F_NEAR_IN + f_in_len / 2.0)
    .rect(W - 2 * F_WALL + 2 * REB_DEPTH, f_in_len + 2 * REB_DEPTH)
    .extrude(FZ1 - REB_Z + 1)
    .edges("|Z")
    .fillet(R_F_IN + REB_DEPTH)
)
for sx in (-1, 1):
    for (yw, d) in ((F_NEAR_IN, 1), (f_far_in, -1)):
        xa = sx * REB_X_END
        xb = sx * (hw + 1.0)
        ya = yw - d * (REB_DEPTH + 1.0)
        yb = yw + d * REB_Y_LEN
        corner_box = (
            cq.Workplane("XY")
            .workplane(offset=REB_Z)
            .center((xa + xb) / 2.0, (ya + yb) / 2.0)
            .rect(abs(xb - xa), abs(yb - ya))
            .extrude(FZ1 - REB_Z + 1)
        )
        body = body.cut(reb_outline.intersect(corner_box))

# ---------------- frame corner bosses ----------------
for sx in (-1, 1):
    for (yw, d) in ((F_NEAR_IN, 1), (f_far_in, -1)):
        y_end = yw + d * BOSS_LEN
        y_root = yw - d * BOSS_ROOT
        # plan shape: rectangle with rounded free-end corners
        plan = (
            cq.Workplane("XY")
            .workplane(offset=BOSS_BOT - 0.5)
            .center(sx * BOSS_X, (y_end + y_root) / 2.0)
            .rect(BOSS_W, abs(y_end - y_root))
            .extrude(BOSS_TOP - BOSS_BOT + 1.0)
        )
        end_sel = ">Y" if d > 0 else "<Y"
        plan = plan.edges("|Z and " + end_sel).fillet(BOSS_R)
        # side profile: chamfered bottom at the free end
        side = (
            cq.Workplane("YZ", origin=(sx * BOSS_X - BOSS_W, 0, 0))
            .polyline([
                (y_root, BOSS_BOT),
                (y_end - d * BOSS_CH_H, BOSS_BOT),
                (y_end, BOSS_BOT + BOSS_CH_V),
                (y_end, BOSS_TOP),
                (y_root, BOSS_TOP),
            ])
            .close()
            .extrude(2 * BOSS_W)
        )
        b = plan.intersect(side)
        # sloped ramp from the boss top up to the rebate floor at the wall
        ramp = (
            cq.Workplane("YZ", origin=(sx * BOSS_X - BOSS_W / 2.0, 0, 0))
            .polyline([
                (yw - d * 0.01, BOSS_TOP - 0.01),
                (yw + d * REB_SLOPE, BOSS_TOP - 0.01),
                (yw - d * 0.01, REB_Z + 0.01),
            ])
            .close()
            .extrude(BOSS_W)
        )
        body = body.union(b).union(ramp)
        hy = yw + d * BOSS_HOLE_OFF
        body = body.cut(
            cq.Workplane("XY").workplane(offset=BOSS_BOT - 1).center(sx * BOSS_X, hy)
            .circle(BOSS_HOLE / 2).extrude(BOSS_TOP - BOSS_BOT + 2)
        )

# ---------------- V notch in the +X frame wall ----------------
notch = (
    cq.Workplane("YZ", origin=(hw - F_WALL - 1.0, 0, 0))
    .polyline([
        (NOTCH_Y - NOTCH_BOT_W / 2.0, FZ1 - NOTCH_D),
        (NOTCH_Y + NOTCH_BOT_W / 2.0, FZ1 - NOTCH_D),
        (NOTCH_Y + NOTCH_TOP_W / 2.0, FZ1 + 0.01),
        (NOTCH_Y + NOTCH_TOP_W / 2.0 + 1.0, FZ1 + 1.0),
        (NOTCH_Y - NOTCH_TOP_W / 2.0 - 1.0, FZ1 + 1.0),
        (NOTCH_Y - NOTCH_TOP_W / 2.0, FZ1 + 0.01),
    ])
    .close()
    .extrude(F_WALL + 2.0)
)
body = body.cut(notch)

result = body
